import math
import cadquery as cq

# ---------------------------------------------------------------------------
# Tilted cover: a wedge-shaped base whose flat top plate is tilted ALPHA
# about Y (rising toward +X) over a flat floor, a raised rounded "nose" cap
# over the front, and blind mounting holes in the plate.
# Modelled in a local frame (u = X, v = Y, w = Z; plate top at w = 0, walls
# normal to the plate), then tilted into place and trimmed at the floor.
# ---------------------------------------------------------------------------

ALPHA = 15.0          # plate tilt, degrees
Z_LEFT = 5.6          # plate top above the floor at the left (-X) edge
H_CAP = 20.5          # nose cap height above the plate (at the step)
BASE_DEPTH = 70.0     # local prism depth below the plate (trimmed by floor)

# ---- plan outline (local u, v) -------------------------------------------
V_BACK_L = 221.4                     # back-left corner
U_RIGHT = 146.1                      # straight right edge
V_BACK_R = 223.5                     # back-right corner
BACK_PTS = [(40.0, 230.3), (95.0, 236.3), (130.3, 232.3)]   # back edge
NOTCH_IN = (U_RIGHT, 159.3)          # concave notch corner
NOTCH_TIP = (177.0, 135.4)           # convex notch tip
FRONT_U = 60.7                       # front-most point of the nose (u)
FRONT_BL = 66.9                      # front/left ellipse semi-axes
FRONT_AR = 68.0                      # front/right ellipse semi-axis (u)
R_BACK_L = 1.5
R_BACK_R = 1.5
R_NOTCH_IN = 14.0
R_NOTCH_TIP = 3.0

# ---- step between plate and nose cap ---------------------------------------
V_STEP = 120.8        # straight part of the step (left of the jog)
U_JOG = 76.0          # jog position
V_JOG = 100.0         # lower end of the jog
STEP_MID = (104.4, 97.0)  # point on the curved part of the step
V_STEP_R = 81.0       # where the curved step meets the lower diagonal edge
R_JOG = 3.0

# ---- nose cap ------------------------------------------------------------------
# Smooth cap lofted through sections at u = CAP_U.  Along the front it rises
# out of the nose wall with a vertical tangent at height wb(u) (a hair outside
# the outline) and rolls over to the flat crest:
#   w = wb + (H_CAP - wb) * g(s),  s = (v - v0(u)) / (vc(u) - v0(u)) in [0, 1],
#   g(s) = (1 - (1 - s)^P_EXP)^(1/Q_EXP).
# v0 follows the nose outline (CAP_MARGIN outside it) and, past U_CREASE,
# pulls away in front of the lower diagonal so the cap meets that wall with a
# crease up to the step; wb and the crest line vc are cubics through the knots.
CAP_KNOTS_U = [0.0, 50.0, 100.0, 146.4]
CAP_WB = [10.0, 0.5, 3.0, 12.0]
CREST_LINE = [105.0, 60.0, 50.0, 75.0]
P_EXP = 1.5
Q_EXP = 1.3
U_CREASE = 128.0
CREASE_K = 1.0
CAP_MARGIN = 0.8
CAP_U = [-2.0, 25.0, 50.0, 75.0, 100.0, 125.0, 151.0]   # loft stations
CAP_S = [0.0, 0.01, 0.04, 0.09, 0.16, 0.25, 0.36, 0.49, 0.64, 0.8, 0.92, 1.0]  # profile samples

# ---- holes (local u, v), blind, normal to the plate -------------------------
HOLE_D = 4.5
HOLE_DEPTH = 3.0
HOLES = [
    (4.3, 218.0), (60.8, 230.5), (118.2, 229.7), (141.2, 220.6),
    (29.3, 193.7), (117.2, 198.0), (29.3, 149.7), (117.2, 153.5),
    (142.8, 164.8), (156.9, 144.4), (171.6, 134.1), (136.3, 122.7),
    (145.0, 86.4), (80.0, 103.4), (4.6, 125.8),
]

# ---------------------------------------------------------------------------
EC = (FRONT_U, FRONT_BL)  # centre of both front ellipse arcs


def _ellipse_tangent_from(p):
    """Parametric angle of the lower right-hand tangent point on the
    front/right ellipse seen from p."""
    def f(t):
        px, py = EC[0] + FRONT_AR * math.cos(t), EC[1] + FRONT_BL * math.sin(t)
        tx, ty = -FRONT_AR * math.sin(t), FRONT_BL * math.cos(t)
        return (px - p[0]) * ty - (py - p[1]) * tx
    lo, hi = -math.pi / 2 + 1e-6, 0.0
    for _ in range(80):
        mid = 0.5 * (lo + hi)
        if f(lo) * f(mid) <= 0:
            hi = mid
        else:
            lo = mid
    return 0.5 * (lo + hi)


T_ANG = _ellipse_tangent_from(NOTCH_TIP)
T_PT = (EC[0] + FRONT_AR * math.cos(T_ANG), EC[1] + FRONT_BL * math.sin(T_ANG))


def diag_u(v):
    return T_PT[0] + (v - T_PT[1]) * (NOTCH_TIP[0] - T_PT[0]) / (NOTCH_TIP[1] - T_PT[1])


B_PT = (diag_u(V_STEP_R), V_STEP_R)  # right end of the step on the diagonal
LEFT_T = (0.0, EC[1])              # ellipse meets the left edge


def V(p, z=0.0):
    return cq.Vector(p[0], p[1], z)


def front_edges():
    """Front of the nose as one smooth curve: an elliptical quarter on the left
    (tangent to the left edge) blending at the front-most point into a wider
    elliptical arc on the right (tangent to the lower diagonal edge)."""
    pts, tans = [], []
    t_end = 360.0 + math.degrees(T_ANG)
    angles = [(180.0, FRONT_U), (200.0, FRONT_U), (220.0, FRONT_U), (240.0, FRONT_U),
              (255.0, FRONT_U), (270.0, FRONT_U), (285.0, FRONT_AR), (300.0, FRONT_AR),
              (315.0, FRONT_AR), (t_end, FRONT_AR)]
    for deg, a in angles:
        t = math.radians(deg)
        pts.append(cq.Vector(EC[0] + a * math.cos(t), EC[1] + FRONT_BL * math.sin(t), 0))
        tans.append(cq.Vector(-a * math.sin(t), FRONT_BL * math.cos(t), 0).normalized())
    return [cq.Edge.makeSpline(pts, tangents=tans)]


def outline_face():
    edges = [
        cq.Edge.makeLine(V(LEFT_T), V((0.0, V_BACK_L))),
        cq.Edge.makeSpline([V((0.0, V_BACK_L))] + [V(p) for p in BACK_PTS]
                           + [V((U_RIGHT, V_BACK_R))]),
        cq.Edge.makeLine(V((U_RIGHT, V_BACK_R)), V(NOTCH_IN)),
        cq.Edge.makeLine(V(NOTCH_IN), V(NOTCH_TIP)),
        cq.Edge.makeLine(V(NOTCH_TIP), V(T_PT)),
    ] + front_edges()
    return cq.Face.makeFromWires(cq.Wire.assembleEdges(edges))


def dome_face():
    edges = [
        cq.Edge.makeLine(V(LEFT_T), V((0.0, V_STEP))),
        cq.Edge.makeLine(V((0.0, V_STEP)), V((U_JOG, V_STEP))),
        cq.Edge.makeLine(V((U_JOG, V_STEP)), V((U_JOG, V_JOG))),
        cq.Edge.makeThreePointArc(V((U_JOG, V_JOG)), V(STEP_MID), V(B_PT)),
        cq.Edge.makeLine(V(B_PT), V(T_PT)),
    ] + front_edges()
    return cq.Face.makeFromWires(cq.Wire.assembleEdges(edges))


def prism(face, z0, z1):
    return cq.Workplane("XY").add(
        cq.Solid.extrudeLinear(face, cq.Vector(0, 0, z1 - z0)).translate((0, 0, z0)))


def fillet_vertical(wp, pts_r):
    for p, r in pts_r:
        sel = cq.selectors.NearestToPointSelector((p[0], p[1], -0.5))
        wp = wp.edges("|Z").edges(sel).fillet(r)
    return wp


# ---- base prism ------------------------------------------------------------
base = prism(outline_face(), -BASE_DEPTH, 0.0)
base = fillet_vertical(base, [
    ((0.0, V_BACK_L), R_BACK_L),
    ((U_RIGHT, V_BACK_R), R_BACK_R),
    (NOTCH_IN, R_NOTCH_IN),
    (NOTCH_TIP, R_NOTCH_TIP),
])


# ---- nose cap: loft of u-stations through the height field -----------------
def _cubic(xs, ys):
    """Lagrange cubic through four knots."""
    def f(x):
        tot = 0.0
        for i in range(4):
            term = ys[i]
            for j in range(4):
                if j != i:
                    term *= (x - xs[j]) / (xs[i] - xs[j])
            tot += term
        return tot
    return f


def front_v(u):
    """v of the nose outline (front ellipses, then the lower diagonal)."""
    u = max(u, 0.0)
    if u <= FRONT_U:
        return EC[1] - FRONT_BL * math.sqrt(max(0.0, 1.0 - ((FRONT_U - u) / FRONT_U) ** 2))
    if u <= T_PT[0]:
        return EC[1] - FRONT_BL * math.sqrt(max(0.0, 1.0 - ((u - FRONT_U) / FRONT_AR) ** 2))
    return T_PT[1] + (u - T_PT[0]) * (NOTCH_TIP[1] - T_PT[1]) / (NOTCH_TIP[0] - T_PT[0])


def v_zero(u):
    return front_v(u) - CAP_MARGIN - CREASE_K * max(0.0, u - U_CREASE)


w_base = _cubic(CAP_KNOTS_U, CAP_WB)
v_crest = _cubic(CAP_KNOTS_U, CREST_LINE)
V_FAR = 135.0
W_LOW = -2.0


def g(s):
    return (1.0 - (1.0 - s) ** P_EXP) ** (1.0 / Q_EXP)


def dg(s):
    a = 1.0 - (1.0 - s) ** P_EXP
    if a <= 0.0:
        return 1e6
    return (1.0 / Q_EXP) * a ** (1.0 / Q_EXP - 1.0) * P_EXP * (1.0 - s) ** (P_EXP - 1.0)


def cap_section(u):
    """Closed section in the plane u = const: rises with a vertical tangent at
    (v0, wb), rolls over to the crest, then runs flat at H_CAP past the step."""
    v0, vc, wb = v_zero(u), v_crest(u), w_base(u)
    prof, tans = [], []
    for s in CAP_S:
        prof.append(cq.Vector(u, v0 + s * (vc - v0), wb + (H_CAP - wb) * g(s)))
        tans.append(cq.Vector(0.0, vc - v0, (H_CAP - wb) * dg(s)).normalized())
    for vv in (vc + 0.5 * (V_FAR - vc), V_FAR):
        prof.append(cq.Vector(u, vv, H_CAP))
        tans.append(cq.Vector(0, 1, 0))
    params = list(CAP_S) + [1.5, 2.0]  # same parametrisation for every station
    e_top = cq.Edge.makeSpline(prof, tangents=tans, parameters=params)
    edges = [
        e_top,
        cq.Edge.makeLine(prof[-1], cq.Vector(u, V_FAR, W_LOW)),
        cq.Edge.makeLine(cq.Vector(u, V_FAR, W_LOW), cq.Vector(u, v0, W_LOW)),
        cq.Edge.makeLine(cq.Vector(u, v0, W_LOW), prof[0]),
    ]
    return cq.Wire.assembleEdges(edges)


loft = cq.Solid.makeLoft([cap_section(u) for u in CAP_U], False)
dome = prism(dome_face(), -1.0, H_CAP + 1.0)
dome = fillet_vertical(dome, [((U_JOG, V_STEP), R_JOG), ((U_JOG, V_JOG), R_JOG)])
cap = dome.intersect(cq.Workplane("XY").add(loft))

body = base.union(cap)

# ---- holes -------------------------------------------------------------------
holes = None
for hu, hv in HOLES:
    c = cq.Workplane("XY").circle(HOLE_D / 2).extrude(HOLE_DEPTH + 1.0).translate(
        (hu, hv, -HOLE_DEPTH))
    holes = c if holes is None else holes.union(c)
body = body.cut(holes)

# ---- tilt into place and trim at the floor ------------------------------------
body = body.rotate((0, 0, 0), (0, 1, 0), -ALPHA).translate((0, 0, Z_LEFT))
floor_box = cq.Workplane("XY").box(600, 600, 300, centered=(True, True, False)).translate((80, 100, 0))
result = body.intersect(floor_box).solids()

VIEW = {"azimuth": 45, "elevation": 26}
